import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
COL_D = 15.8          # column outer diameter
BORE_D = 9.0          # through bore (also the centre hole of the plate)
H_TOTAL = 237.3       # column bottom to plate top

PLATE_L = 68.4        # plate length (X)
PLATE_W = 30.4        # plate width (Y)
PLATE_T = 7.4         # plate thickness
PLATE_R = 6.5         # plate corner radius (plan view)
SMALL_HOLE_D = 4.5    # 4 mounting holes
SMALL_HOLE_PITCH = 15.2

ARM_T = 15.7          # arm (ring) height
ARM_OFFSET = 19.6     # centre of the ring's outer arc from the column axis (+Y)
RING_RO = 14.1        # ring outer radius
HOLE_OFFSET = 18.7    # centre of the ring hole from the column axis (+Y)
RING_RI = 10.75       # ring hole radius
ARM_Z = [0.0, 76.3, 137.5]   # arm bottom heights
COLLAR_STEP = 0.25    # upper arms' collar stands slightly proud of the column

GX_T = 8.0            # thickness of the rib running along X (long plate axis)
GY_T = 6.8            # thickness of the rib running along Y
# gusset profiles: (radial offset from axis, depth below plate bottom)
RC = COL_D / 2
GX_PTS = [(30.6, 0.0), (28.4, 6.2), (23.3, 11.2), (16.4, 15.4), (10.3, 18.6), (RC - 0.3, 20.0)]
GX_END_TAN = (-0.89, -0.45)
GY_PTS = [(14.2, 0.0), (14.0, 7.5), (12.7, 13.4), (10.3, 18.0), (RC - 0.3, 21.0)]
GY_END_TAN = (-0.55, -0.83)

Z_PB = H_TOTAL - PLATE_T   # plate bottom

# ---------------- column ----------------
# (seam of the cylindrical face placed on the +Y side, toward the arms)
column = cq.Workplane(cq.Plane((0, 0, 0), (0, 1, 0), (0, 0, 1))).circle(RC).extrude(Z_PB + 0.5)

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY", origin=(0, 0, Z_PB))
    .rect(PLATE_L, PLATE_W)
    .extrude(PLATE_T)
    .edges("|Z").fillet(PLATE_R)
)

body = column.union(plate)


# ---------------- arms: hull of column circle and ring circle ----------------
def arm_solid(z0, collar_r):
    r1, r2, d = collar_r, RING_RO, ARM_OFFSET
    ny = (r1 - r2) / d
    nx = math.sqrt(1 - ny * ny)
    t1r = (r1 * nx, r1 * ny)
    t2r = (r2 * nx, d + r2 * ny)
    t1l = (-t1r[0], t1r[1])
    t2l = (-t2r[0], t2r[1])
    prof = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(*t1r)
        .lineTo(*t2r)
        .threePointArc((0, d + r2), t2l)
        .lineTo(*t1l)
        .threePointArc((0, -r1), t1r)
        .close()
        .extrude(ARM_T)
    )
    hole = cq.Workplane("XY", origin=(0, HOLE_OFFSET, z0 - 1)).circle(RING_RI).extrude(ARM_T + 2)
    return prof.cut(hole)


for i, z in enumerate(ARM_Z):
    body = body.union(arm_solid(z, RC if i == 0 else RC + COLLAR_STEP))


# ---------------- gussets (cross ribs) under the plate ----------------
def gusset(pts, end_tan, plane_name, offset_dir, thick):
    # profile drawn in a vertical plane: local x = radial direction, local y = Z
    ox, oy = offset_dir
    wp = cq.Workplane(plane_name, origin=(ox * thick / 2, oy * thick / 2, 0))
    top = Z_PB + 0.5
    spl = [(p[0], Z_PB - p[1]) for p in pts]
    prof = (
        wp.moveTo(0, top)
        .lineTo(pts[0][0], top)
        .lineTo(*spl[0])
        .spline(spl[1:], tangents=[(0, -1), end_tan], includeCurrent=True)
        .lineTo(0, spl[-1][1])
        .close()
    )
    return prof.extrude(thick)


# XZ plane normal is -Y, so start at +Y side and extrude toward -Y
gx = gusset(GX_PTS, GX_END_TAN, "XZ", (0, 1), GX_T)
gx = gx.union(gx.mirror("YZ"))
# YZ plane normal is +X, so start at -X side and extrude toward +X
gy = gusset(GY_PTS, GY_END_TAN, "YZ", (-1, 0), GY_T)
gy = gy.union(gy.mirror("XZ"))
body = body.union(gx).union(gy)

# ---------------- holes ----------------
body = body.cut(cq.Workplane("XY", origin=(0, 0, -1)).circle(BORE_D / 2).extrude(H_TOTAL + 2))
p = SMALL_HOLE_PITCH / 2
small = (
    cq.Workplane("XY", origin=(0, 0, Z_PB - 1))
    .pushPoints([(p, p), (-p, p), (p, -p), (-p, -p)])
    .circle(SMALL_HOLE_D / 2)
    .extrude(PLATE_T + 2)
)
body = body.cut(small)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
